import math
import cadquery as cq
from OCP.gp import gp_GTrsf
from OCP.BRepBuilderAPI import BRepBuilderAPI_GTransform

# ---------------------------------------------------------------------------
# Game-controller lower housing: open shell made of a rounded central body and
# two spheroidal handle lobes, rim with a locating lip, internal screw bosses,
# an H-shaped post, a battery tray in the left handle, plus seven loose pins.
# Driving dimensions are in "units"; U converts units to millimetres.
# ---------------------------------------------------------------------------
U = 0.75                        # mm per unit

# central body
BODY_HX = 73.5                  # half length (X)
BODY_Y0, BODY_Y1 = -37.5, 36.8  # front / back (Y)
BODY_RC = 30.0                  # plan-view corner radius
BODY_RH = 19.0                  # bottom rounding, horizontal reach
BODY_EX, BODY_EZ = 76.0, 13.0   # elliptical belly across the width; rounding height

# rim plane: Z = RIM_Z0 - RIM_K * (Y - BODY_Y0)  (tilts down toward the handles)
RIM_Z0 = 21.6
RIM_K = 0.1207
RIM_ANG = math.degrees(math.atan(RIM_K))

WALL = 2.6                      # shell wall
FLOOR_Z = 2.6                   # inside floor height at the centre
LIP_H = 1.0                     # rim lip height
LIP_W = 1.1                     # rim lip width

# handle lobes (prolate spheroids, centre above the rim plane)
LOBE_CX, LOBE_CY = 73.3, 28.9
LOBE_DZ = 10.0                  # centre height above the rim plane
LOBE_A, LOBE_R = 54.8, 24.5     # semi-axis along the handle, radius across
LOBE_YAW = 13.9                 # deg, tips turned outward
LOBE_PITCH = 14.5               # deg, tips dropped


def gscale(shape, sx, sy, sz):
    gt = gp_GTrsf()
    gt.SetValue(1, 1, sx)
    gt.SetValue(2, 2, sy)
    gt.SetValue(3, 3, sz)
    return cq.Shape.cast(BRepBuilderAPI_GTransform(shape.wrapped, gt, True).Shape())


def rim_z(y):
    return RIM_Z0 - RIM_K * (y - BODY_Y0)


def box(cx, cy, sx, sy, z0, z1):
    return cq.Workplane("XY").workplane(offset=z0).center(cx, cy).rect(sx, sy).extrude(z1 - z0)


def body_solid(inset, z0):
    """rounded plan-view block with an elliptical bottom rounding (fillet made in
    a vertically stretched space) and an elliptical belly across the width"""
    zc = BODY_EZ
    y0, y1 = BODY_Y0 + inset, BODY_Y1 - inset
    f = BODY_RH / zc                             # stretch factor for the fillet
    rf = BODY_RH - inset
    b = (cq.Workplane("XY")
         .sketch().rect(2 * (BODY_HX - inset), y1 - y0).vertices().fillet(BODY_RC - inset)
         .finalize().extrude(60.0 * f))
    b = b.faces("<Z").edges().fillet(rf)
    s = gscale(b.val(), 1, 1, 1.0 / f).translate(cq.Vector(0, (y0 + y1) / 2, z0))
    # belly across the width
    ex, ez = BODY_EX - inset, zc - z0
    bx = cq.Workplane("XZ").center(0, zc).ellipse(ex, ez).extrude(100, both=True)
    bx = bx.union(box(0, 0, 2 * ex, 200, zc, zc + 60))
    return s.intersect(bx.val())


def lobe_solid(side, inset):
    a, r = LOBE_A - inset, LOBE_R - inset
    e = (cq.Workplane("XY").ellipseArc(r, a, angle1=-90, angle2=90, startAtCurrent=False)
         .close().revolve(360, (0, -1, 0), (0, 1, 0)).val())
    e = e.rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), -LOBE_PITCH)
    e = e.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), LOBE_YAW * side)
    return e.translate(cq.Vector(-side * LOBE_CX, LOBE_CY, rim_z(LOBE_CY) + LOBE_DZ))


def envelope(inset, z0):
    return body_solid(inset, z0).fuse(lobe_solid(1, inset), lobe_solid(-1, inset)).clean()


def above_rim(dz=0.0, thick=80.0):
    big = cq.Solid.makeBox(400, 400, thick, cq.Vector(-200, -200, 0))
    big = big.rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), -RIM_ANG)
    return big.translate(cq.Vector(0, BODY_Y0, RIM_Z0 + dz))


def W(shape):
    return cq.Workplane("XY").add(shape)


def floor_z(x, y):
    """approximate height of the inside floor surface at (x, y)"""
    ex = BODY_EX - WALL
    zx = BODY_EZ - (BODY_EZ - FLOOR_Z) * math.sqrt(max(0.0, 1 - (x / ex) ** 2))
    rv = BODY_EZ - FLOOR_Z
    zy = FLOOR_Z
    for dist, r in ((y - (BODY_Y0 + WALL), BODY_RH - WALL), ((BODY_Y1 - WALL) - y, BODY_RH - WALL)):
        if dist < r:
            dy = r - max(dist, 0.0)
            zy = max(zy, FLOOR_Z + rv * (1 - math.sqrt(max(0.0, 1 - (dy / r) ** 2))))
    return max(zx, zy)


def post(x, y, z_top, d, z0=None):
    if z0 is None:   # reach the lowest floor point under the footprint (clipped later)
        h = d / 2
        z0 = min(floor_z(x + sx * h, y + sy * h) for sx in (-1, 0, 1) for sy in (-1, 0, 1)) - 0.8
    return cq.Workplane("XY").workplane(offset=z0).center(x, y).circle(d / 2).extrude(z_top - z0)


# ---------------------------------------------------------------------------
# shell: outer skin up to the rim, a lip band on the inner half of the wall
# ---------------------------------------------------------------------------
outer = envelope(0.0, 0.0)
inner = envelope(WALL, FLOOR_Z)
lipenv = envelope(WALL - LIP_W, FLOOR_Z - 0.8)

shell = (outer.cut(above_rim(0.0))
         .fuse(lipenv.cut(above_rim(LIP_H)))
         .cut(inner))

# ---------------------------------------------------------------------------
# left-handle battery tray: raised block with two pockets and a contact pin
# ---------------------------------------------------------------------------
TRAY = dict(cx=-73.6, cy=24.4, ang=29.0, w=13.0, l=38.0, depth=4.0, top=13.0)    # long pocket
BOX = dict(cx=-78.9, cy=58.5, ang=37.0, w=14.7, l=25.0, depth=3.8, top=10.0)     # end pocket
TRAY_WALL = 2.2
TRAY_PIN = (-82.0, 39.5, 16.8)


def rrect(d, grow, h0, h1):
    return (cq.Workplane("XY").workplane(offset=h0).center(d["cx"], d["cy"])
            .rect(d["w"] + 2 * grow, d["l"] + 2 * grow).extrude(h1 - h0)
            .rotate((d["cx"], d["cy"], 0), (d["cx"], d["cy"], 1), d["ang"]))


LOBE_FILL_Z = 8.5              # raised floor inside the left handle
fill = box(-LOBE_CX, LOBE_CY, 80, 140, -10, LOBE_FILL_Z).cut(W(body_solid(WALL, FLOOR_Z)))
blk = rrect(TRAY, TRAY_WALL, -5, TRAY["top"]).union(rrect(BOX, TRAY_WALL, -5, BOX["top"]))
blk = blk.union(fill).intersect(W(lobe_solid(1, WALL)))
for d in (TRAY, BOX):
    blk = blk.cut(rrect(d, 0.0, d["top"] - d["depth"], d["top"] + 1))
blk = blk.union(post(TRAY_PIN[0], TRAY_PIN[1], TRAY_PIN[2], 1.6,
                     z0=TRAY["top"] - TRAY["depth"] - 0.5))

# ---------------------------------------------------------------------------
# internal bosses: (x, y, top z, diameter, kind)
#   kind: "hole" = screw boss, "disk" = plain pad, "cut" = boss with a notch
# ---------------------------------------------------------------------------
BOSS_HOLE = 1.6
bosses = [
    (-46.5, 20.9, 19.5, 6.0, "hole"), (-26.3, 20.9, 19.1, 6.0, "hole"),
    (-10.1, 20.9, 5.9, 7.5, "hole"), (6.1, 20.9, 5.9, 7.5, "hole"),
    (22.3, 20.9, 19.0, 6.0, "hole"), (41.2, 20.9, 19.2, 6.5, "hole"),
    (-11.9, 9.2, 7.3, 6.5, "cut"), (7.0, 9.2, 6.7, 6.5, "cut"),
    (-46.5, -1.2, 18.9, 6.0, "hole"), (-27.2, -1.2, 19.5, 6.0, "hole"),
    (22.3, -1.2, 19.0, 6.0, "hole"), (40.8, -1.2, 19.5, 6.0, "hole"),
    (-9.2, -5.7, 11.7, 6.0, "hole"), (6.6, -5.7, 12.1, 6.0, "hole"),
    (-8.6, 31.2, 10.7, 7.0, "disk"), (5.2, 31.2, 13.3, 7.0, "cut"),
]
feat = None


def add(f):
    global feat
    feat = f if feat is None else feat.union(f)


for (x, y, zt, dia, kind) in bosses:
    b = post(x, y, zt, dia)
    if kind == "hole":
        b = b.faces(">Z").workplane().hole(BOSS_HOLE, 6.0)
    elif kind == "cut":
        b = b.cut(box(x + dia / 4, y + dia / 4, dia / 2, dia / 2, zt - 3.0, zt + 1.0))
    add(b)

# rib between the two low pads and a clip on the back wall
add(box(-2.0, 20.9, 16.0, 1.2, 1.8, 4.6))
add(box(-1.6, 32.5, 3.0, 2.5, 7.0, 12.5))

# three small rounded cups near the front
for x in (-24.1, -5.6, 11.5):
    add(box(x, -16.0, 12.6, 10.8, 1.8, 11.0).edges("|Z").fillet(2.2).faces(">Z").shell(-1.0))

# flat panel with a foot ledge and a divider rib on the inside of the front wall
PANEL_X0, PANEL_X1 = -30.0, 18.0
PANEL_Z0 = 7.0
PANEL_Z1 = rim_z(-33.6) - 2.5
pcx = (PANEL_X0 + PANEL_X1) / 2
add(box(pcx, -33.2, PANEL_X1 - PANEL_X0, 3.2, PANEL_Z0, PANEL_Z1))
add(box(pcx, -30.8, PANEL_X1 - PANEL_X0, 2.0, PANEL_Z0, PANEL_Z0 + 2.5))
add(box(-4.0, -30.8, 1.2, 2.4, PANEL_Z0, PANEL_Z1))

# tab on the front wall, rising just above the rim
add(box(19.5, -34.2, 5.0, 2.6, 8.0, rim_z(-34.0) + 1.6))

# H-shaped post (front right), standing above the rim
HX, HY = 45.6, -11.9
H_TOP = 32.3
H_T = 3.4
add(post(HX, HY, H_TOP - H_T + 0.1, 6.2))
add(cq.Workplane("XY").workplane(offset=H_TOP - H_T)
    .pushPoints([(HX - 7.6, HY), (HX + 7.6, HY)]).rect(4.0, 16.0).extrude(H_T))
add(box(HX, HY, 12.0, 5.0, H_TOP - H_T, H_TOP - 1.2))     # cross bar sits a little lower

# side window (vertical slot) through the outer right-hand boss
feat = feat.cut(cq.Workplane("YZ").workplane(offset=36.0).center(20.9, 13.9)
                .slot2D(7.2, 3.6, angle=90).extrude(10))

# keep the features inside the outer skin of the central body
feat = feat.intersect(W(body_solid(0.0, 0.0)))

# ---------------------------------------------------------------------------
# loose pins (thin rods): (x, y, top z); all share the same bottom height
# ---------------------------------------------------------------------------
PIN_D = 0.8
PIN_BOT = -5.3
pins = [
    (-29.2, 44.0, 24.6), (138.25, 46.0, 25.0),
    (-11.9, -65.0, 6.5), (0.6, -65.0, 6.5), (20.6, -65.0, 6.5),
    (7.4, -32.6, 4.0), (29.9, -32.6, 4.0),
]
pin_solids = [post(x, y, zt, PIN_D, z0=PIN_BOT).val() for (x, y, zt) in pins]

# ---------------------------------------------------------------------------
# assemble, then the front-wall window, the rim notch and the back-wall window
# ---------------------------------------------------------------------------
WIN_X, WIN_Z, WIN_W, WIN_H = -52.0, 15.2, 9.8, 6.2
BACK_SLOT = (-11.0, 5.5, 9.4, 11.4)     # x from, x to, z from, z to of the back-wall window
NOTCH_X, NOTCH_W, NOTCH_D = 23.5, 4.6, 2.8
win = cq.Workplane("XZ").workplane(offset=45).center(WIN_X, WIN_Z).rect(WIN_W, WIN_H).extrude(-15)
notch = (cq.Workplane("XZ").workplane(offset=45).center(NOTCH_X, rim_z(BODY_Y0))
         .rect(NOTCH_W, 2 * NOTCH_D).extrude(-12))

body = shell.fuse(blk.val(), feat.val()).clean()
slot = box((BACK_SLOT[0] + BACK_SLOT[1]) / 2, BODY_Y1 + 3.0, BACK_SLOT[1] - BACK_SLOT[0], 13.0,
           BACK_SLOT[2], BACK_SLOT[3])
body = body.cut(win.val().fuse(notch.val(), slot.val()))
part = body.fuse(*pin_solids)

result = W(part.scale(U))
